import math
import cadquery as cq
from OCP.gp import gp_GTrsf, gp_Mat, gp_XYZ
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform, BRepBuilderAPI_Sewing, BRepBuilderAPI_MakeSolid
from OCP.TopoDS import TopoDS
from OCP.ShapeFix import ShapeFix_Solid

# ============ driving dimensions (mm) ============
# Balloon-like body hanging below a hoop hanger, with a partial band around it,
# a knot + string under the body and a small detached clip far below.

# ---- body: union of overlapping ellipsoid lobes (centre xyz, semi-axes xyz)
BODY_LOBES = [
    ((-27.7, 33.2, 17.0), (42.6, 31.0, 37.6)),   # main lobe
    ((-37.7, 31.9, 28.8), (31.9, 30.8, 27.9)),   # squared-off crown
    ((-4.6, 31.8, 36.5), (19.6, 22.1, 24.3)),    # upper right lump
    ((-41.6, 34.4, 14.0), (32.6, 32.0, 28.6)),   # full left flank
    ((-53.3, 49.8, 15.9), (17.1, 16.3, 21.7)),   # rear left shoulder
    ((-47.6, 16.3, 16.2), (21.4, 14.5, 28.1)),   # front left shoulder
    ((-6.8, 30.3, 0.4), (15.1, 10.8, 16.2)),     # lower right bulge (knot side)
]
STUB_XZ = (-9.5, 30.5)            # small peg on the -Y flank
STUB_Y0, STUB_Y1 = 10.0, -6.8
STUB_D = 6.0

# ---- hoop hanger with central post
RING_C = (-25.2, 30.2)
RING_RO = 20.5
RING_T = 2.0                       # radial wall
RING_Z0, RING_H = 111.2, 5.5
POST_D = 8.7
LUG_ANGLES = (-62.0, 62.0)        # small lugs standing on the hoop (deg about +Z)
LUG_W, LUG_T, LUG_RISE = 3.0, 2.4, 1.5
POST_Z0, POST_Z1 = 85.2, 110.8

# ---- partial band (large circular strip) around the body
ARC_C = (-25.8, 32.5)
ARC_R = 103.0                      # centre-line radius
ARC_W = 1.3                        # radial width
ARC_H = 2.4                        # height
ARC_ZC = 69.5                      # mid height
ARC_A0, ARC_A1 = 47.4, 144.4       # start / end angle (deg, about +Z from +X)
ARC_GAPS = [(68.2, 1.6), (99.2, 2.0), (119.7, 1.6), (133.5, 2.4)]  # (angle, width deg)

# ---- knot (flat ribbon) and string below the body, in the plane Y = KNOT_Y
KNOT_Y = 30.0
KNOT_T = 1.8
KNOT_PTS = [(-4.8, -11.0), (5.4, -13.5), (9.2, -27.7), (6.1, -39.2), (-16.2, -29.2)]
STRING_D = 1.8
STRING_PTS = [(6.5, -38.0), (9.0, -46.0), (6.9, -52.3), (3.8, -61.5), (-1.5, -67.7), (-6.2, -71.5)]

# ---- small detached clip: bent plate with a wire tail, plus a loose pin
CLIP_P0 = (103.8, -135.3)          # plate corner (tail side)
CLIP_P1 = (109.4, -131.2)          # plate far edge
CLIP_Z0, CLIP_Z1 = -107.6, -98.6
CLIP_T = 1.2
TAIL_TOP = (103.8, -135.0, -107.0)
TAIL_BOT = (99.2, -129.4, -117.6)
TAIL_D = 1.2
PIN_XY = (88.8, -126.0)
PIN_Z0, PIN_Z1 = -107.7, -102.0
PIN_D = 1.2


def ellipsoid(c, r):
    """Triaxial ellipsoid: a unit sphere scaled non-uniformly, built from two half
    surfaces sewn into one closed shell (keeps every face un-closed / un-periodic)."""
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(r[0], 0, 0, 0, r[1], 0, 0, 0, r[2]))
    g.SetTranslationPart(gp_XYZ(*c))
    sew = BRepBuilderAPI_Sewing(1e-6)
    for a0 in (0, 180):
        half = cq.Solid.makeSphere(
            1.0, cq.Vector(0, 0, 0), cq.Vector(0, 1, 0),
            angleDegrees1=-90, angleDegrees2=90, angleDegrees3=180,
        ).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), a0)
        half = cq.Shape.cast(BRepBuilderAPI_GTransform(half.wrapped, g, True).Shape())
        dome = max(half.Faces(), key=lambda f: f.Area())
        sew.Add(dome.wrapped)
    sew.Perform()
    solid = BRepBuilderAPI_MakeSolid(TopoDS.Shell_s(sew.SewedShape())).Solid()
    fix = ShapeFix_Solid(solid)
    fix.Perform()
    return cq.Solid(fix.Solid())


# ================= body =================
body_shape = None
for c, r in BODY_LOBES:
    e = ellipsoid(c, r)
    body_shape = e if body_shape is None else body_shape.fuse(e).clean()
body = cq.Workplane("XY").add(body_shape)

stub = (
    cq.Workplane("XZ", origin=(0, STUB_Y0, 0))      # XZ normal is -Y
    .center(STUB_XZ[0], STUB_XZ[1])
    .circle(STUB_D / 2)
    .extrude(STUB_Y0 - STUB_Y1)
)

# ================= knot + string =================
knot = (
    cq.Workplane("XZ", origin=(0, KNOT_Y + KNOT_T / 2, 0))
    .polyline(KNOT_PTS).close()
    .extrude(KNOT_T)
)
path = cq.Workplane("XZ", origin=(0, KNOT_Y, 0)).spline(STRING_PTS, includeCurrent=False)
s0 = STRING_PTS[0]
string = (
    cq.Workplane(cq.Plane(origin=(s0[0], KNOT_Y, s0[1]), xDir=(1, 0, 0), normal=(0, 0, -1)))
    .circle(STRING_D / 2)
    .sweep(path)
)
body = body.union(stub).union(knot).union(string)

# ================= hoop hanger + post =================
hoop = (
    cq.Workplane("XY", origin=(RING_C[0], RING_C[1], RING_Z0))
    .circle(RING_RO).circle(RING_RO - RING_T)
    .extrude(RING_H)
)
post = (
    cq.Workplane("XY", origin=(RING_C[0], RING_C[1], POST_Z0))
    .circle(POST_D / 2)
    .extrude(POST_Z1 - POST_Z0)
)


for a in LUG_ANGLES:
    lug = (
        cq.Workplane("XY")
        .box(LUG_T, LUG_W, RING_H + LUG_RISE, centered=(True, True, False))
        .translate((RING_RO - RING_T / 2, 0, RING_Z0))
        .rotate((0, 0, 0), (0, 0, 1), a)
        .translate((RING_C[0], RING_C[1], 0))
    )
    hoop = hoop.union(lug)


# ================= partial band =================
def band_segment(a0, a1):
    r_in = ARC_R - ARC_W / 2
    seg = (
        cq.Workplane("XZ")
        .center(r_in, ARC_ZC - ARC_H / 2)
        .rect(ARC_W, ARC_H, centered=False)
        .revolve(a1 - a0, (-r_in, 0, 0), (-r_in, 1, 0))     # about the global Z axis
    )
    return seg.rotate((0, 0, 0), (0, 0, 1), a0).translate((ARC_C[0], ARC_C[1], 0))


cuts = [ARC_A0]
for a, g in ARC_GAPS:
    cuts += [a - g / 2, a + g / 2]
cuts.append(ARC_A1)
band = None
for i in range(0, len(cuts), 2):
    seg = band_segment(cuts[i], cuts[i + 1])
    band = seg if band is None else band.union(seg)


# ================= detached clip =================
def plate(p, q, z0, z1, t):
    dx, dy = q[0] - p[0], q[1] - p[1]
    length = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    mid = ((p[0] + q[0]) / 2, (p[1] + q[1]) / 2, (z0 + z1) / 2)
    return (
        cq.Workplane("XY")
        .box(length, t, z1 - z0)
        .rotate((0, 0, 0), (0, 0, 1), ang)
        .translate(mid)
    )


clip = plate(CLIP_P0, CLIP_P1, CLIP_Z0, CLIP_Z1, CLIP_T)
tail_vec = cq.Vector(TAIL_BOT) - cq.Vector(TAIL_TOP)
tail = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(TAIL_D / 2, tail_vec.Length, cq.Vector(TAIL_TOP), tail_vec.normalized())
)
clip = clip.union(tail)
pin = (
    cq.Workplane("XY", origin=(PIN_XY[0], PIN_XY[1], PIN_Z0))
    .circle(PIN_D / 2)
    .extrude(PIN_Z1 - PIN_Z0)
)

# ================= assemble (separate bodies, as in the reference) =================
parts = [body, hoop, post, band, clip, pin]
solids = [s for p in parts for s in p.solids().vals()]
result = cq.Workplane("XY").add(cq.Compound.makeCompound(solids))

VIEW = {"azimuth": 45, "elevation": 26}
